import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 56.0          # overall width  (X)
L = 96.5          # overall length (Y)
T = 1.95          # top plate thickness
C_TOP = 1.2       # top outer edge chamfer, vertical leg
C_TOP_H = 0.7     # top outer edge chamfer, horizontal leg
C_BOT = 0.6       # chamfer on lip bottom edge
R_BACK = 1.6      # plan corner radius at +Y end
R_FRONT = 1.5     # plan corner radius at -Y (lip) end
LIP = 12.9        # length of thin front lip (no walls under it)
TW = 1.6          # wall thickness
H_W = 8.2         # depth of perimeter walls below plate top
H_BOSS = 9.3      # depth of standoffs / rails
BOSS_D = 5.3
BOSS_HOLE = 2.4
CSK = 1.05        # countersink (45 deg chamfer) around slots
ENGRAVE = 0.5     # depth of engraved arrows / text
R_CUT = 0.5       # corner radius of plate cut-outs

Y0 = -L / 2 + LIP  # start of walled section
YB = L / 2         # back end


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def prism(pts, z0, z1, r=0.0):
    p = cq.Workplane("XY").polyline(pts).close().extrude(z1 - z0).translate((0, 0, z0))
    if r > 0:
        p = p.edges("|Z").fillet(r)
    return p


def rbox(x0, x1, y0, y1, z0, z1, r=R_CUT):
    b = box(x0, x1, y0, y1, z0, z1)
    if r > 0:
        b = b.edges("|Z").fillet(r)
    return b


# ---------------- top plate ----------------
plate = box(-W / 2, W / 2, -L / 2, L / 2, -T, 0)
plate = plate.edges("|Z and >Y").fillet(R_BACK).edges("|Z and <Y").fillet(R_FRONT)
plate = plate.faces(">Z").edges().chamfer(C_TOP, C_TOP_H)
plate = plate.faces("<Z").edges().chamfer(C_BOT)

# ---------------- perimeter walls (open toward the lip) ----------------
outer = box(-W / 2, W / 2, Y0, YB, -H_W, -C_TOP - 0.05)
outer = outer.edges("|Z and >Y").fillet(R_BACK)
inner = box(-W / 2 + TW, W / 2 - TW, Y0 - 1, YB - TW, -H_W - 1, 0)
inner = inner.edges("|Z and >Y").fillet(R_BACK - 0.6)
walls = outer.cut(inner)

body = plate.union(walls)

# shallow stiffening rib across the underside at the start of the walled section
RIB_H = 0.5
body = body.union(box(-W / 2 + TW - 0.1, W / 2 - TW + 0.1, Y0 + 0.25, Y0 + 1.45, -T - RIB_H, -T + 0.1))

# locating tongue along the inner bottom edge of both side walls
TONGUE_T = 0.6
H_TONGUE = 9.1    # depth of tongue below plate top
TONGUE_GAP = (-18.5, -13.0)   # interruption of the tongues
for sx in (1, -1):
    xa, xb = sorted((sx * (W / 2 - TW), sx * (W / 2 - TW + TONGUE_T)))
    y_start = Y0 + 0.5 if sx < 0 else TONGUE_GAP[1]
    tongue = box(xa, xb, y_start, YB - TW, -H_TONGUE, -T + 0.1)
    tongue = tongue.cut(box(xa - 1, xb + 1, TONGUE_GAP[0], TONGUE_GAP[1], -H_BOSS - 1, -H_W + 0.01))
    body = body.union(tongue)

# ---------------- standoffs / corner blocks ----------------
B1 = (-5.2, -31.0)     # free standing standoff
B2 = (23.7, -31.4)     # boss at front end of +X wall
B3 = (24.0, 43.2)      # hole in +X/+Y corner block
B4 = (-24.0, 43.2)     # hole in -X/+Y corner block
BLK_IN = 21.1          # inner x-face of corner blocks (abs)
BLK_Y = 39.85          # front face of corner blocks


def standoff(x, y, flare=0.0):
    """revolved standoff: chamfered foot, optional flared root under the plate"""
    r = BOSS_D / 2
    pts = [(0, -H_BOSS), (r - 0.4, -H_BOSS), (r, -H_BOSS + 0.4)]
    if flare > 0:
        pts += [(r, -T - flare), (r + flare, -T + 0.05)]
    else:
        pts += [(r, -T + 0.05)]
    pts += [(0, -T + 0.05)]
    s = cq.Workplane("XZ").polyline(pts).close().revolve(360, (0, 0, 0), (0, 1, 0))
    return s.translate((x, y, 0))


body = body.union(standoff(*B1, flare=0.8))
body = body.union(standoff(*B2))
# tie B2 to the +X wall
body = body.union(box(B2[0], W / 2 - TW + 0.1, B2[1] - BOSS_D / 2, B2[1] + BOSS_D / 2, -H_BOSS, -1.5))

for sx in (1, -1):
    xa, xb = sorted((sx * BLK_IN, sx * (W / 2 - TW)))
    body = body.union(box(xa, xb, BLK_Y, YB - TW, -H_BOSS, -1.0))

for (bx, by) in (B1, B2, B3, B4):
    h = cq.Workplane("XY").circle(BOSS_HOLE / 2).extrude(H_BOSS - T - 0.6).translate((bx, by, -H_BOSS - 0.1))
    body = body.cut(h)


# ---------------- notches in the walls ----------------
def notch_y(x0, x1, ztop, r):
    c = box(x0, x1, YB - TW - 2.0, YB + 1, -H_BOSS - 1, ztop)
    return c.edges("|Y and >Z").fillet(r)


body = body.cut(notch_y(11.6, 22.6, -5.0, 2.0))      # +Y wall, notch A
body = body.cut(notch_y(-2.0, 7.9, -5.0, 2.0))       # +Y wall, notch B
body = body.cut(notch_y(-20.0, -8.2, -6.7, 0.6))     # +Y wall, shallow notch

# notch through the +X wall (leaves a thin strip at the bottom)
body = body.cut(box(W / 2 - TW - 1.0, W / 2 + 1, -11.15, 1.8, -7.3, 1))

# ---------------- through cut-outs in plate ----------------
ZC0, ZC1 = -T - 0.5, 1.0


def countersunk(b, tool, x0, x1, y0, y1, c):
    """cut a through opening and chamfer its top edge (countersunk slot)"""
    b = b.cut(tool)
    sel = cq.selectors.BoxSelector((x0 - 0.05, y0 - 0.05, -0.05), (x1 + 0.05, y1 + 0.05, 0.05))
    return b.edges(sel).chamfer(c)


# left long slot with stepped lower end
body = body.cut(prism([(-24.72, 32.02), (-16.93, 32.02), (-16.93, 4.2), (-19.30, 4.2),
                       (-19.30, 1.44), (-26.4, 1.44), (-26.4, 4.4), (-24.72, 4.4)],
                      ZC0, ZC1, 0.4))
# big window with tab
body = body.cut(prism([(-14.20, 24.1), (14.18, 24.1), (14.18, 33.2), (7.12, 33.2),
                       (7.12, 35.56), (-0.46, 35.56), (-0.46, 33.2), (-14.20, 33.2)],
                      ZC0, ZC1, R_CUT))
# right long slot (runs into the +X wall notch)
body = body.cut(prism([(22.29, 36.34), (W / 2 - TW, 36.34), (W / 2 - TW, -11.08), (18.86, -11.08),
                       (18.86, 1.44), (16.93, 1.44), (16.93, 32.02), (22.29, 32.02)],
                      ZC0, ZC1, 0.4))
# small countersunk hole near right slot
body = countersunk(body, rbox(13.5, 16.05, 17.75, 20.85, ZC0, ZC1, 0.0), 13.5, 16.05, 17.75, 20.85, 0.8)
# small rounded slot at left
body = body.cut(rbox(-26.35, -16.08, -3.62, -0.68, ZC0, ZC1, 0.6))
# left edge notch, continues as a channel down the -X wall
body = body.cut(rbox(-27.04, -20.48, -18.54, -14.54, -H_BOSS - 1, ZC1, 0.3))
# square hole
body = body.cut(rbox(-12.0, -6.21, -24.45, -16.78, ZC0, ZC1, 0.4))
# front-left countersunk slot
body = countersunk(body, rbox(-25.73, -11.43, -33.46, -30.96, ZC0, ZC1, 0.0),
                   -25.73, -11.43, -33.46, -30.96, CSK)
# countersunk obround slot in the lip
sl = cq.Workplane("XY").slot2D(16.5, 3.0).extrude(ZC1 - ZC0).translate((0.0, -36.66, ZC0))
body = countersunk(body, sl, -8.25, 8.25, -38.16, -35.16, CSK)


# ---------------- engraved arrows ----------------
def arrow(cx, cy):
    pts = [(-3.78, 1.03), (-0.24, 1.03), (-1.72, 2.79), (0.73, 2.79), (3.87, 0.0),
           (0.73, -2.79), (-1.72, -2.79), (-0.24, -1.03), (-3.78, -1.03)]
    a = prism([(cx + x, cy + y) for (x, y) in pts], -ENGRAVE, 1.0)
    return a.edges("|Z").edges("<X").fillet(0.4)


for cx in (-19.8, 19.86):
    body = body.cut(arrow(cx, -40.0))

# ---------------- engraved text ----------------
try:
    txt = (cq.Workplane("XY")
           .text("Prog", 5.3, -ENGRAVE, kind="regular", halign="center", valign="bottom")
           .translate((3.14, 41.64, 0)))
    body = body.cut(txt)
except Exception:
    pass

result = body
